import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
H = 40.0                      # overall height (Z)
EDGE_R = 0.6                  # small edge round-over

# front plate (faces -Y)
FP_X0, FP_X1 = 28.4, 71.1
FP_T = 6.0

# thick right block behind the front plate
TB_X0, TB_X1 = 55.8, 78.4
TB_Y1 = 13.25
TB_R = 3.2                    # rounded front-right vertical edge

# left band (faces -Y, set back)
BAND_Y0, BAND_Y1 = 8.5, 13.9
JUNC_X1 = 31.0

# web joining band and left wall
WEB_X0, WEB_X1 = 8.7, 14.0
WEB_TOP_Y = 23.8
WALL_JOIN_Y = 29.6
GUS = 5.0                     # top gusset in the band/web inner corner
GUS_Z0 = 30.0

# left wall (runs along Y at the back-left)
WALL_T = 8.7
WALL_Y0, WALL_Y1 = 25.0, 53.3

# recess on the +X face of the left wall (smooth 45 deg ramps)
REC_X = 3.7
REC_ZA, REC_ZD = 8.8, 34.7

# notch through the front plate
N_X0, N_X1, N_Z = 33.1, 55.7, 17.1
RAIL_X = 34.5
RAIL_Z0, RAIL_Z1 = 3.0, 8.6
RRAIL_X, RRAIL_Z0, RRAIL_Z1 = 55.0, 1.9, 8.2
SW_X0, SW_H = 54.4, 8.5

# channel blocks behind the notch
CB_H = 16.1
LCB_X0, LCB_X1, LCB_HX0, LCB_Y1, LCB_CH = 25.1, 33.1, 22.9, 32.2, 7.4
LCB_BV = 3.5
FOOT_X0, FOOT_Y1, FOOT_H = 14.0, 17.2, 12.8
RCB_X1, RCB_Y1, RCB_CH = 63.8, 25.1, 5.6
HEAD_X0, HEAD_Y1, HEAD_H, HEAD_CH = 51.3, 29.9, 11.0, 4.7
HEAD_CX, HEAD_CZ = 3.4, 3.4

# cavity under the thick block (behind the plain hole)
CAV_X1, CAV_Z0, CAV_Z = 62.0, 17.0, 27.5

# holes
CB1_DEPTH = 4.0              # counterbore depth of the upper front hole
XH_Z = 5.4
XH1_Y, XH2_Y = 4.0, 18.8
XH_D, XH_CB_D = 3.9, 7.6

# hexagon logo on the outer (-X) face of the left wall
HEX_YC, HEX_ZC, HEX_R, HEX_D = 36.6, 21.0, 12.2, 0.6
SL_ANG, SL_LONG, SL_SHORT, SL_W, SL_OFF = 131.0, 17.0, 9.5, 1.45, 4.4


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


def fil_z(wp, x, y, r, z=H / 2):
    """fillet the vertical edge nearest to (x, y, z)"""
    return wp.edges("|Z").edges(cq.selectors.NearestToPointSelector((x, y, z))).fillet(r)


def cyl_y(x, z, d, y0, y1):
    return (cq.Workplane("XZ").center(x, z).circle(d / 2).extrude(-(y1 - y0))
            .translate((0, y0, 0)))


def cyl_x(y, z, d, x0, x1):
    return cq.Workplane("YZ").center(y, z).circle(d / 2).extrude(x1 - x0).translate((x0, 0, 0))


def cyl_z(x, y, d, z0, z1):
    return cq.Workplane("XY").center(x, y).circle(d / 2).extrude(z1 - z0).translate((0, 0, z0))


# ---------------- main plan profile, full height ----------------
plan = [
    (0, BAND_Y0), (FP_X0, BAND_Y0), (FP_X0, 0), (FP_X1, 0), (FP_X1, FP_T),
    (TB_X1, FP_T), (TB_X1, TB_Y1), (TB_X0, TB_Y1), (TB_X0, FP_T), (JUNC_X1, FP_T),
    (JUNC_X1, BAND_Y1), (WEB_X1, BAND_Y1),
    (WEB_X1, WEB_TOP_Y), (WALL_T, WALL_JOIN_Y), (WALL_T, WALL_Y1), (0, WALL_Y1),
    (0, WALL_Y0), (WEB_X0, WALL_Y0), (WEB_X0, BAND_Y1), (0, BAND_Y1),
]
body = cq.Workplane("XY").polyline(plan).close().extrude(H)

body = fil_z(body, TB_X1, FP_T, TB_R)
body = fil_z(body, 0, BAND_Y0, 1.6)
body = fil_z(body, JUNC_X1, BAND_Y1, 1.6)
body = fil_z(body, WEB_X1, WEB_TOP_Y, 3.0)
body = fil_z(body, WALL_T, WALL_JOIN_Y, 3.5)
body = fil_z(body, WEB_X1, BAND_Y1, 0.5)
body = fil_z(body, TB_X1, TB_Y1, 0.6)
body = fil_z(body, FP_X1, 0, 0.5)
body = fil_z(body, FP_X0, 0, 0.6)
body = fil_z(body, 0, WALL_Y1, 0.6)
body = fil_z(body, WALL_T, WALL_Y1, 0.6)
# top gusset in the inner corner between band and web
gus = (cq.Workplane("XY")
       .polyline([(WEB_X1 - 0.5, BAND_Y1 - 0.5), (WEB_X1 + GUS, BAND_Y1 - 0.5),
                  (WEB_X1 + GUS, BAND_Y1), (WEB_X1, BAND_Y1 + GUS), (WEB_X1 - 0.5, BAND_Y1 + GUS)])
       .close().extrude(H - GUS_Z0).translate((0, 0, GUS_Z0)))
body = body.union(gus)

# small round-over on the top and bottom outline edges
body = body.faces(">Z").edges().fillet(EDGE_R)
body = body.faces("<Z").edges().fillet(EDGE_R)


# ---------------- recess on +X face of the left wall ----------------
# one smooth spline profile (X, Z): upper lip, 45 deg ramp, recessed face, 45 deg ramp, lower lip
_k = math.sqrt(0.5)
_dz = WALL_T - REC_X
rec_pts = [(WALL_T - _dz / 2, REC_ZD - 0.7 * _dz), (REC_X, REC_ZD - 1.42 * _dz),
           (REC_X, REC_ZA + 1.44 * _dz), (WALL_T - _dz / 2, REC_ZA + 0.7 * _dz), (WALL_T, REC_ZA)]
rec_tan = [(0, -1), (-_k, -_k), (0, -1), (0, -1), (_k, -_k), (0, -1)]
rec = (cq.Workplane("XZ")
       .moveTo(WALL_T + 3, REC_ZD).lineTo(WALL_T, REC_ZD)
       .spline(rec_pts, tangents=rec_tan, includeCurrent=True)
       .lineTo(WALL_T + 3, REC_ZA)
       .close()
       .extrude(-(WALL_Y1 + 1 - (WALL_JOIN_Y + 1.2)))
       .translate((0, WALL_JOIN_Y + 1.2, 0)))
body = body.cut(rec)

# ---------------- notch through the front plate ----------------
notch_pts = [
    (N_X0, -1), (N_X0, RAIL_Z0), (RAIL_X, RAIL_Z0), (RAIL_X, RAIL_Z1), (N_X0, RAIL_Z1),
    (N_X0, N_Z), (N_X1, N_Z), (N_X1, -1),
]
notch = (cq.Workplane("XZ").polyline(notch_pts).close().extrude(-(FP_T + 2.0))
         .translate((0, -0.5, 0)))
body = body.cut(notch)

# small rail on the right side of the notch
body = body.union(box(RRAIL_X, N_X1 + 0.2, -0.0, FP_T, RRAIL_Z0, RRAIL_Z1))

# ---------------- channel blocks behind the notch ----------------
lcb = box(LCB_X0, LCB_X1, BAND_Y1 - 0.5, LCB_Y1, 0, CB_H)
lcb = lcb.union(box(LCB_HX0, LCB_X1, RCB_Y1, LCB_Y1, 0, CB_H))
lcb = lcb.union(box(JUNC_X1 - 0.5, LCB_X1, FP_T - 0.5, BAND_Y1, 0, CB_H))
lcb = lcb.edges("|X and >Y and >Z").chamfer(LCB_CH)
# bevel along the top -X edge of the left channel block
lbev = (cq.Workplane("XZ").polyline([(LCB_HX0 - 1, CB_H - LCB_BV - 1), (LCB_HX0 + LCB_BV + 1, CB_H + 1),
                                      (LCB_HX0 - 1, CB_H + 1)]).close()
        .extrude(-(LCB_Y1 + 2 - BAND_Y1)).translate((0, BAND_Y1, 0)))
lcb = lcb.cut(lbev)
lcb = lcb.union(box(LCB_X1 - 0.5, RAIL_X, FP_T - 0.5, LCB_Y1 - LCB_CH, RAIL_Z0, RAIL_Z1))
lcb = lcb.union(box(FOOT_X0, LCB_X0 + 0.5, BAND_Y1 - 0.5, FOOT_Y1, 0, FOOT_H))
body = body.union(lcb)

# pocket behind the plain hole, open to the back of the thick block
cav = box(TB_X0 - 1, CAV_X1, FP_T, TB_Y1 + 1, CAV_Z0, CAV_Z)
cav = cav.edges("|Y and >Z and >X").chamfer(3.0)
body = body.cut(cav)

rcb = box(TB_X0, RCB_X1, TB_Y1 - 0.5, RCB_Y1, 0, CB_H)
rcb = rcb.edges("|X and >Y and >Z").chamfer(RCB_CH)
body = body.union(rcb)
head = (cq.Workplane("XZ")
        .polyline([(HEAD_X0, 0), (RCB_X1, 0), (RCB_X1, HEAD_H), (HEAD_X0 + HEAD_CX, HEAD_H),
                   (HEAD_X0, HEAD_H - HEAD_CZ)])
        .close().extrude(-(HEAD_Y1 - RCB_Y1 + 0.5)).translate((0, RCB_Y1 - 0.5, 0)))
head = head.edges("|Z and >X and >Y").chamfer(HEAD_CH)
head = head.faces(">Z").edges(">X or >Y").chamfer(1.2)
body = body.union(head)
# blind counterbored hole in the back face of the head
body = body.cut(cyl_y(57.3, 5.0, 3.4, HEAD_Y1 - 9, HEAD_Y1 + 1))
body = body.cut(cyl_y(57.3, 5.0, 6.0, HEAD_Y1 - 1.0, HEAD_Y1 + 1))
# thin side wall along the channel
sw = box(SW_X0, TB_X0 + 0.3, FP_T - 0.3, RCB_Y1, 0, SW_H)
sw = sw.edges("|Y and >Z and <X").chamfer(0.8)
body = body.union(sw)

# ---------------- holes ----------------
# counterbored hole through front plate + thick block (upper right)
body = body.cut(cyl_y(60.0, 35.8, 4.1, -1, TB_Y1 + 1))
body = body.cut(cyl_y(60.0, 35.8, 7.5, -1, CB1_DEPTH))
# plain hole with counterbore on the back face of the front plate
body = body.cut(cyl_y(55.0, 23.6, 7.7, -1, FP_T + 1))
body = body.cut(cyl_y(55.0, 23.6, 10.5, FP_T - 1.2, FP_T + 3))
# blind holes on the back of the thick block
body = body.cut(cyl_y(73.0, 35.5, 3.0, TB_Y1 - 6, TB_Y1 + 1))
body = body.cut(cyl_y(74.0, 6.5, 3.0, TB_Y1 - 5, TB_Y1 + 1))
# nut slot in the back of the thick block
body = body.cut(box(65.0, 69.0, TB_Y1 - 5, TB_Y1 + 1, 13.2, 24.4))

# vertical counterbored holes from the top
for (hx, hy) in [(66.6, 4.4), (12.9, 12.3)]:
    body = body.cut(cyl_z(hx, hy, 3.1, H - 16, H + 1))
    body = body.cut(cyl_z(hx, hy, 5.8, H - 2.0, H + 1))
# vertical hole from below in the foot
body = body.cut(cyl_z(21.8, 14.6, 3.2, -1, 10))
body = body.cut(cyl_z(21.8, 14.6, 6.0, -1, 2.0))

# holes along X near the bottom
body = body.cut(cyl_x(XH1_Y, XH_Z, XH_D, FP_X0 - 1, TB_X1 + 1))
cb = cyl_x(XH1_Y, XH_Z, XH_CB_D, FP_X1 - 1.5, FP_X1 + 3.0)
cb = cb.union(cq.Workplane("XY").sphere(XH_CB_D / 2).translate((FP_X1 + 3.0, XH1_Y, XH_Z)))
body = body.cut(cb)
body = body.cut(cyl_x(XH2_Y, XH_Z, 4.1, WEB_X0 - 1, RCB_X1 + 1))
body = body.cut(cyl_x(XH2_Y, XH_Z, 7.4, RCB_X1 - 2.0, RCB_X1 + 1))
# small holes in the web (along X)
for hz in (23.9, 16.9):
    body = body.cut(cyl_x(15.0, hz, 2.2, WEB_X1 - 5, WEB_X1 + 1))

# holes along Y through the left wall, ending blind in the band
for hz in (36.0, 6.0):
    body = body.cut(cyl_y(WALL_T / 2, hz, 3.0, 10.0, WALL_Y1 + 1))

# window through the left band
body = body.cut(box(13.5, 21.7, BAND_Y0 - 1, BAND_Y1 + 1, 10.8, 28.1))

# slot on top of the left wall
body = body.cut(box(1.3, 2.5, 28.3, 44.9, H - 4, H + 1))

# ---------------- hexagon logo on the -X face of the left wall ----------------
hex_pts = [(HEX_YC + HEX_R * math.cos(math.radians(90 + 60 * i)),
            HEX_ZC + HEX_R * math.sin(math.radians(90 + 60 * i))) for i in range(6)]
hexa = cq.Workplane("YZ").polyline(hex_pts).close().extrude(HEX_D + 1).translate((-1, 0, 0))
body = body.cut(hexa)
# slashes (viewed from -X they read as "/"), parallelogram shaped
ang = math.radians(SL_ANG)
ux, uy = math.cos(ang), math.sin(ang)          # along the slash (in Y, Z)
px, py = -uy, ux                               # across the slash
for off, ln in ((0.0, SL_LONG), (SL_OFF, SL_SHORT), (-SL_OFF, SL_SHORT)):
    cy = HEX_YC + off * px
    cz = HEX_ZC + off * py
    hl, hw = ln / 2, SL_W / 2
    # ends cut parallel to Y
    dy_end = hw / abs(py) if abs(py) > 1e-6 else hw
    pts = [(cy - hl * ux - dy_end, cz - hl * uy), (cy - hl * ux + dy_end, cz - hl * uy),
           (cy + hl * ux + dy_end, cz + hl * uy), (cy + hl * ux - dy_end, cz + hl * uy)]
    sl = cq.Workplane("YZ").polyline(pts).close().extrude(HEX_D + 1.0).translate((-0.5, 0, 0))
    body = body.cut(sl)

result = body
